import math
import cadquery as cq

# ---------------- driving dimensions (mm) ----------------
D = 100.0            # outer diameter
H = 47.0             # overall height
TOP_CH = 1.7         # chamfer on the top outer edge

# D-shaped bore from the top
BORE_R = 35.25       # bore radius
FLAT_Y = -25.6       # the flat of the D (towards -Y / front)

# ledges (floor of the bore) with a conical transition to the bore wall
LEDGE_Z = 23.55      # height of the flat top of the ledges
LEDGE_CH_W = 4.8     # radial width of the conical (45 deg) transition
LEDGE_CH_H = 4.8     # rise of the conical transition

# T-shaped opening through the ledge floor (down to the bottom face)
STEM_X0 = -11.6      # stem left edge
STEM_X1 = 8.6        # stem right edge
LEDGE_Y_TOP = 8.8    # top (+Y) edge of the ledges
STEP_Y = -8.3        # step between the narrow stem and the wide part

# annular groove in the bottom face (leaves a central hub)
GROOVE_RI = 38.25    # 3 mm hub wall around the bore
GROOVE_RO = 47.0     # 3 mm outer skin
GROOVE_DEPTH = 44.0   # the groove leaves a 3 mm top wall: thin-walled shell

# two screw holes at the front: a clearance hole through the outer skin and a
# counterbored hole from the groove through the hub into the flat of the bore
HOLE_X = (-11.0, 11.0)
HOLE_Z = H - 12.5
SKIN_HOLE_D = 12.7   # hole through the outer skin
SPOT_CLEAR = 0.2     # the counterbore floor cleans up the hub surface by this much
CB_D = 9.3           # countersink diameter on that floor
POINT_ANGLE = 90.0   # countersink included angle
HOLE_D = 4.7         # small hole through the hub into the bore

SEAM_ANGLE = 67.5    # where the outer periodic faces get their seam (near the silhouettes)
GROOVE_SEAM = 45.0   # seam of the groove walls (on the silhouette of the underside view)

VIEW = {"azimuth": 45, "elevation": 26}


def rot(shape_wp, angle=SEAM_ANGLE):
    """turn a rotationally symmetric tool so its seam sits at the given angle"""
    return shape_wp.rotate((0, 0, 0), (0, 0, 1), angle)


# ---------------- body: cylinder with edge chamfers ----------------
body = rot(
    cq.Workplane("XY")
    .circle(D / 2)
    .extrude(H)
    .faces(">Z").edges().chamfer(TOP_CH)
)

# ---------------- D-shaped bore from the top ----------------
HALF_CHORD = math.sqrt(BORE_R ** 2 - FLAT_Y ** 2)
WIDE_HALF = HALF_CHORD  # the wide part of the T spans the whole flat


def d_profile(wp):
    return (
        wp.moveTo(-HALF_CHORD, FLAT_Y)
        .lineTo(HALF_CHORD, FLAT_Y)
        .threePointArc((0, BORE_R), (-HALF_CHORD, FLAT_Y))
        .close()
    )


bore_bottom = LEDGE_Z + LEDGE_CH_H
bore = d_profile(cq.Workplane("XY").workplane(offset=bore_bottom)).extrude(H - bore_bottom + 1)
body = body.cut(bore)

# conical transition between bore wall and the ledge top (revolved cutter, kept behind the flat)
r_in = BORE_R - LEDGE_CH_W
cone = rot(
    cq.Workplane("XZ")
    .polyline([(0, LEDGE_Z), (r_in, LEDGE_Z), (BORE_R, bore_bottom), (0, bore_bottom)])
    .close()
    .revolve(360, (0, 0, 0), (0, 1, 0))
)
behind_flat = cq.Workplane("XY").box(2 * D, 2 * D, 2 * H).translate((0, FLAT_Y + D, 0))
body = body.cut(cone.intersect(behind_flat))

# ---------------- annular groove in the bottom ----------------
groove = rot(cq.Workplane("XY").circle(GROOVE_RO).circle(GROOVE_RI).extrude(GROOVE_DEPTH), GROOVE_SEAM)
body = body.cut(groove)

# ---------------- through opening below the ledges ----------------
# circular segment of the bore beyond the ledges
upper = d_profile(cq.Workplane("XY").workplane(offset=-1)).extrude(H + 2).intersect(
    cq.Workplane("XY").box(2 * D, D, 4 * H).translate((0, LEDGE_Y_TOP + D / 2, 0))
)
# narrow stem of the T
stem = (
    cq.Workplane("XY").workplane(offset=-1)
    .center((STEM_X0 + STEM_X1) / 2, (STEP_Y + LEDGE_Y_TOP) / 2 + 0.5)
    .rect(STEM_X1 - STEM_X0, LEDGE_Y_TOP - STEP_Y + 1)
    .extrude(H + 2)
)
# wide part of the T along the flat
wide = (
    cq.Workplane("XY").workplane(offset=-1)
    .center(0, (FLAT_Y + STEP_Y) / 2)
    .rect(2 * WIDE_HALF, STEP_Y - FLAT_Y)
    .extrude(H + 2)
)
body = body.cut(upper).cut(stem).cut(wide)

# ---------------- holes in the front ----------------
for hx in HOLE_X:
    # counterbore through the outer skin, continued into the hub down to a flat floor
    # that just cleans up the curved hub surface over the whole counterbore diameter
    SPOT_Y = -math.sqrt(GROOVE_RI ** 2 - (abs(hx) + SKIN_HOLE_D / 2) ** 2) + SPOT_CLEAR
    cbore = (
        cq.Workplane("XZ", origin=(hx, -D / 2 - 5, HOLE_Z))
        .circle(SKIN_HOLE_D / 2)
        .extrude(-(SPOT_Y - (-D / 2 - 5)))
    )
    # 90 deg countersink on the floor and the small hole into the bore
    k = math.tan(math.radians(POINT_ANGLE / 2))
    extra = 0.5
    r_top = CB_D / 2 + extra * k
    cs_len = (r_top - HOLE_D / 2) / k
    csk = cq.Workplane("XY").add(
        cq.Solid.makeCone(r_top, HOLE_D / 2, cs_len,
                          cq.Vector(hx, SPOT_Y - extra, HOLE_Z), cq.Vector(0, 1, 0))
    )
    small = (
        cq.Workplane("XZ", origin=(hx, SPOT_Y - 1, HOLE_Z))
        .circle(HOLE_D / 2)
        .extrude(-(FLAT_Y + 3 - (SPOT_Y - 1)))
    )
    body = body.cut(cbore).cut(csk).cut(small)

result = body
